"""Smart-watch style case: rounded body with band slots at both ends, two side
buttons on each long side, a micro-USB style port and a stepped cavity in the
underside."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 36.0          # body width  (X)
L = 48.0          # body length (Y)
H = 12.0          # body height (Z)
R_PLAN = 5.2      # plan-view corner radius
R_TOP = 4.3       # top edge roundover
R_BOT = 1.7       # bottom edge roundover

# band slot (groove across each Y end)
SLOT_LOW_Z = 8.2      # top of lower body at the ends
SLOT_C_IN = 3.0       # groove circle centre inset from end face
SLOT_C_Z = 8.65       # groove circle centre height
SLOT_R = 1.65         # groove circle radius
LIP_IN = 2.2          # lid lip set back from end face
LIP_LOW_Z = 10.75     # underside of lip at its tip
LID_CA = 4.2          # lid outline corner: semi-axis along X
LID_CB = 2.6          # lid outline corner: semi-axis along Y
LIP_FR = 0.25         # nose rounding of the lip

# side buttons (both X sides, mirrored in Y)
BTN_Y = 12.5
BTN_Z = 3.65
BTN_W = 6.4           # along Y
BTN_H = 5.36          # along Z
BTN_R = 1.4           # corner radius
BTN_BASE = 1.1        # base plate protrusion beyond wall
BTN_NECK = 0.42       # narrow neck between base and cap
BTN_CAP = 1.1         # cap thickness
BTN_ROOT_R = 0.5      # blend between button base and wall

# port on +X side (micro-USB outline)
PORT_Y = -0.47
PORT_Z = 3.93
PORT_L = 8.06
PORT_H = 3.37
PORT_D = 4.5          # cut depth (breaks through into the cavity)
PORT_R = 0.9          # top corner radius
PORT_CH_Y = 1.35      # bottom chamfer along Y
PORT_CH_Z = 1.1       # bottom chamfer along Z

# underside cavity, built from rectangular pockets (x0, x1, y0, y1, depth from bottom)
CAVITY = [
    (-14.3, 14.3, -11.5, 9.4, 4.4),   # main chamber
    (-14.3, 14.3, 9.4, 13.3, 4.8),    # slightly deeper strip
    (-14.3, -7.8, 13.3, 17.2, 4.8),   # corner extension
    (-7.8, 14.3, 13.3, 17.2, 0.25),   # shallow shelf
]

# parting line (small groove around the sides)
PART_Z = 3.5
PART_D = 0.12

# ---------------- main body ----------------
body = (
    cq.Workplane("XY")
    .box(W, L, H, centered=(True, True, False))
    .edges("|Z").fillet(R_PLAN)
    .faces(">Z").edges().fillet(R_TOP)
    .faces("<Z").edges().fillet(R_BOT)
)


# ---------------- band slots at both Y ends ----------------
def groove_cutter(sign):
    """Groove (channel + mouth) profile in the YZ plane for the +Y end, swept along X."""
    yc = L / 2 - SLOT_C_IN
    zc = SLOT_C_Z
    r = SLOT_R

    def pc(a):
        return (yc + r * math.cos(math.radians(a)), zc + r * math.sin(math.radians(a)))

    far = L / 2 + 6
    y_lip = L / 2 - LIP_IN
    top = pc(90)
    slope = (LIP_LOW_Z - top[1]) / (y_lip - top[0])
    wp = (
        cq.Workplane("YZ")
        .moveTo(far, SLOT_LOW_Z)
        .lineTo(L / 2, SLOT_LOW_Z)
        .lineTo(*pc(-60))
        .threePointArc(pc(-150), pc(180))
        .threePointArc(pc(135), top)
        .lineTo(far, top[1] + (far - top[0]) * slope)
        .close()
        .extrude(W, both=True)
    )
    if sign < 0:
        wp = wp.mirror("XZ")
    return wp


# the lid (above the groove) is shorter than the body: rectangle with elliptical corners
LID_L = L - 2 * LIP_IN
lid_prism = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .rect(W + 0.02, LID_L - 2 * LID_CB)
    .extrude(H + 3)
    .union(cq.Workplane("XY", origin=(0, 0, -1)).rect(W + 0.02 - 2 * LID_CA, LID_L).extrude(H + 3))
)
for cx in (1, -1):
    for cy in (1, -1):
        lid_prism = lid_prism.union(
            cq.Workplane("XY", origin=(cx * (W / 2 + 0.01 - LID_CA), cy * (LID_L / 2 - LID_CB), -1))
            .ellipse(LID_CA, LID_CB)
            .extrude(H + 3)
        )
lid_cut = (
    cq.Workplane("XY", origin=(0, 0, SLOT_LOW_Z))
    .rect(W + 10, L + 10)
    .extrude(H)
    .cut(lid_prism)
)
body = body.cut(groove_cutter(1)).cut(groove_cutter(-1)).cut(lid_cut)

# round the nose of the lid lip: fillet the edge loop around the lid end faces
_ylid = L / 2 - LIP_IN
_x0 = W / 2 + 0.01 - LID_CA
_y0 = _ylid - LID_CB


def _on_lid_boundary(p, tol=2e-3):
    ax, ay = abs(p.x), abs(p.y)
    if abs(ay - _ylid) < tol and ax <= _x0 + tol:
        return True
    if ax > _x0 - tol and ay > _y0 - tol:
        v = ((ax - _x0) / LID_CA) ** 2 + ((ay - _y0) / LID_CB) ** 2
        return abs(v - 1) < 5e-3
    return False


_nose = []
for e in body.edges().vals():
    pts = [e.positionAt(t) for t in (0.1, 0.5, 0.9)]
    if all(_on_lid_boundary(p) for p in pts) and min(p.z for p in pts) > SLOT_C_Z + 1.0:
        bb = e.BoundingBox()
        if e.geomType() == "LINE" and (bb.zmax - bb.zmin) > 0.05 and (bb.xmax - bb.xmin) < 1e-3:
            continue  # tangent seam between end face and corner face
        _nose.append(e)

for _r in (LIP_FR, 0.2, 0.15):
    try:
        body = cq.Workplane("XY").add(body.val().fillet(_r, _nose))
        break
    except Exception:
        continue


# ---------------- side buttons ----------------
def rrect_x(x0, thick, w, h, r, y, z):
    """Rounded rectangle plate normal to X starting at x0 extending +thick."""
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center(y, z)
        .rect(w, h)
        .extrude(thick)
        .edges("|X").fillet(r)
    )


def button(by):
    xw = W / 2
    base = rrect_x(xw - 1.0, 1.0 + BTN_BASE, BTN_W, BTN_H, BTN_R, by, BTN_Z)
    base = base.faces(">X").edges().fillet(0.12)
    neck = rrect_x(xw + BTN_BASE - 0.05, BTN_NECK + 0.1, BTN_W - 0.8, BTN_H - 0.8,
                   BTN_R - 0.4, by, BTN_Z)
    cap = rrect_x(xw + BTN_BASE + BTN_NECK, BTN_CAP, BTN_W, BTN_H, BTN_R, by, BTN_Z)
    cap = cap.faces(">X").edges().fillet(0.25).faces("<X").edges().fillet(0.12)
    return base.union(neck).union(cap)


for side in (1, -1):
    for by in (BTN_Y, -BTN_Y):
        btn = button(by)
        if side < 0:
            btn = btn.mirror("YZ")
        body = body.union(btn)


def _rrect_sdf(dy, dz, hw, hh, r):
    qy = abs(dy) - (hw - r)
    qz = abs(dz) - (hh - r)
    outside = math.hypot(max(qy, 0.0), max(qz, 0.0))
    return outside + min(max(qy, qz), 0.0) - r


def _root_edge(e):
    for t in (0.05, 0.35, 0.65, 0.95):
        p = e.positionAt(t)
        if not (W / 2 - 1.0 < abs(p.x) < W / 2 + 0.02):
            return False
        by = BTN_Y if p.y > 0 else -BTN_Y
        if abs(_rrect_sdf(p.y - by, p.z - BTN_Z, BTN_W / 2, BTN_H / 2, BTN_R)) > 0.02:
            return False
    return True


# soft blend where each button base meets the case wall
_roots = [e for e in body.edges().vals() if _root_edge(e)]
for _r in (BTN_ROOT_R, 0.35, 0.25):
    try:
        body = cq.Workplane("XY").add(body.val().fillet(_r, _roots))
        break
    except Exception:
        continue

# ---------------- parting line groove (interrupted at the buttons) ----------------
ring = (
    cq.Workplane("XY", origin=(0, 0, PART_Z))
    .rect(W + 4, L + 4)
    .extrude(PART_D)
    .cut(
        cq.Workplane("XY", origin=(0, 0, PART_Z))
        .rect(W - 2 * PART_D, L - 2 * PART_D)
        .extrude(PART_D)
        .edges("|Z").fillet(R_PLAN - PART_D)
    )
)
for sx in (1, -1):
    for by in (BTN_Y, -BTN_Y):
        ring = ring.cut(
            cq.Workplane("XY", origin=(sx * (W / 2 + 1.5), by, PART_Z - 1))
            .rect(4.0, BTN_W + 2 * BTN_ROOT_R + 0.4)
            .extrude(2)
        )
body = body.cut(ring)

# ---------------- port (micro-USB style) on +X side ----------------
pz0 = PORT_Z - PORT_H / 2
pz1 = PORT_Z + PORT_H / 2
hw = PORT_L / 2
port = (
    cq.Workplane("YZ", origin=(W / 2 - PORT_D, 0, 0))
    .polyline([
        (PORT_Y - hw, pz0 + PORT_CH_Z),
        (PORT_Y - hw + PORT_CH_Y, pz0),
        (PORT_Y + hw - PORT_CH_Y, pz0),
        (PORT_Y + hw, pz0 + PORT_CH_Z),
        (PORT_Y + hw, pz1),
        (PORT_Y - hw, pz1),
    ]).close()
    .extrude(PORT_D + 2)
    .edges("|X").edges(">Z").fillet(PORT_R)
)
body = body.cut(port)


# ---------------- cavity in the underside ----------------
def bottom_pocket(x0, x1, y0, y1, depth):
    return (
        cq.Workplane("XY", origin=(0, 0, -1))
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .rect(x1 - x0, y1 - y0)
        .extrude(1 + depth)
    )


for pk in CAVITY:
    body = body.cut(bottom_pocket(*pk))

result = body
